import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Spiral bevel gear (45 deg pitch cone, 32 curved teeth) with a splined hub.
# Gear axis = Y.  The toothed cone face and the hub point towards -Y, the flat
# back face of the gear is at +Y.
# ---------------------------------------------------------------------------

# --- gear parameters ---------------------------------------------------------
Z_TEETH = 32                  # number of teeth
OUTER_D = 120.0               # tip diameter at the heel
DELTA = math.radians(45.0)    # pitch cone angle
FACE_W = 18.8                 # face width (along the cone)
ADD_F = 1.0                   # addendum   / module (at the heel)
DED_F = 1.15                  # dedendum   / module (at the heel)
PRESSURE = math.radians(16.0)  # normal pressure angle
FLANK_BULGE = 0.6             # convexity of the tooth flanks at the heel (mm)
BETA_M = math.radians(22.0)   # mean spiral angle
CUTTER_R = 80.0               # cutter radius -> curvature of the tooth trace
PHASE = math.radians(1.8)     # angular position of the tooth pattern
TOE_TIP_Y = 0.0               # plane containing the toe tips of the teeth
BACK_LAND = 0.2               # back face offset behind the heel root

# --- hub parameters (towards -Y, measured from the toe-tip plane) ------------
COLLAR_R = 15.3               # plain collar next to the gear
COLLAR_L = 9.4                # visible collar length
NECK_L = 3.9                  # conical neck from collar down to the spline
SPLINE_R = 11.4               # spline crest radius
SPLINE_ROOT_R = 10.3          # spline groove radius
SPLINE_L = 11.3               # splined length
N_SPLINES = 20                # number of rounded spline ridges
FLARE_L = 3.9                 # conical flare out to the end disc
END_R = 15.3                  # end disc radius

# --- derived cone geometry -----------------------------------------------------
MODULE = OUTER_D / (Z_TEETH + 2.0 * ADD_F * math.cos(DELTA))
ADD = ADD_F * MODULE
DED = DED_F * MODULE
sd, cd = math.sin(DELTA), math.cos(DELTA)
A = MODULE * Z_TEETH / (2.0 * sd)       # outer cone distance (heel)
Li = A - FACE_W                          # inner cone distance (toe)
Lm = A - FACE_W / 2.0                    # mean cone distance
k_toe = Li / A
heel_tip_y = A * cd - ADD * sd           # heel tip height above the apex
Y_APEX = TOE_TIP_Y - heel_tip_y * k_toe  # common apex of all cones


def meridian(L, v):
    """(r, y) of the pitch point at cone distance L, offset v along the
    outward cone normal."""
    return (L * sd + v * cd, Y_APEX + L * cd - v * sd)


def pitch_pt(L, th):
    """3D point on the pitch cone at cone distance L and polar angle th."""
    r = L * sd
    return (r * math.cos(th), Y_APEX + L * cd, r * math.sin(th))


def frame(th):
    """tangential direction and outward cone normal at polar angle th."""
    et = (-math.sin(th), 0.0, math.cos(th))
    n = (cd * math.cos(th), -sd, cd * math.sin(th))
    return et, n


def add(p, *terms):
    x, y, z = p
    for s, v in terms:
        x += s * v[0]
        y += s * v[1]
        z += s * v[2]
    return (x, y, z)


# --- spiral tooth trace: circular arc on the developed pitch cone -------------
Cx = Lm + CUTTER_R * math.sin(BETA_M)
Cy = -CUTTER_R * math.cos(BETA_M)


def trace_psi(L):
    """developed angle of the tooth centre line at cone distance L."""
    d = math.hypot(Cx, Cy)
    a = (L * L - CUTTER_R * CUTTER_R + d * d) / (2 * d)
    h = math.sqrt(max(L * L - a * a, 0.0))
    ux, uy = Cx / d, Cy / d
    px, py = a * ux, a * uy
    best = None
    for qx, qy in ((px + h * uy, py - h * ux), (px - h * uy, py + h * ux)):
        ang = math.atan2(qy, qx)
        if best is None or abs(ang) < abs(best):
            best = ang          # branch through the mean point
    return best


def theta_of(L):
    return trace_psi(L) / sd   # developed angle -> polar angle on the gear


ALPHA_T = math.atan(math.tan(PRESSURE) / math.cos(BETA_M))


def tooth_section(L, th0):
    """transverse tooth section (convex flanks) at cone distance L."""
    k = L / A
    s_half = math.pi * MODULE / 4.0 * k
    v_lo = -(DED + 0.6) * k          # slightly below the root (buried)
    v_hi = (ADD + 0.4) * k           # slightly above the tip (trimmed)
    th = th0 + theta_of(L)
    p = pitch_pt(L, th)
    et, n = frame(th)
    ta = math.tan(ALPHA_T)
    w_lo = s_half - v_lo * ta
    w_hi = s_half - v_hi * ta
    v_md = 0.5 * (v_lo + v_hi)
    w_md = s_half - v_md * ta
    bl = FLANK_BULGE * k
    cb, sb = math.cos(ALPHA_T), math.sin(ALPHA_T)

    def P(w, v):
        return cq.Vector(*add(p, (w, et), (v, n)))

    rl, rr = P(-w_lo, v_lo), P(w_lo, v_lo)
    tl, tr = P(-w_hi, v_hi), P(w_hi, v_hi)
    ml = P(-(w_md + bl * cb), v_md + bl * sb)
    mr = P(w_md + bl * cb, v_md + bl * sb)
    return cq.Wire.assembleEdges([
        cq.Edge.makeLine(rl, rr),
        cq.Edge.makeThreePointArc(rr, mr, tr),
        cq.Edge.makeLine(tr, tl),
        cq.Edge.makeThreePointArc(tl, ml, rl),
    ])


def make_tooth(th0):
    """one curved tooth lofted through transverse sections toe -> heel."""
    Ls = [Li - 1.5, Li + FACE_W * 0.25, Lm, A - FACE_W * 0.25, A + 1.5]
    return cq.Solid.makeLoft([tooth_section(L, th0) for L in Ls], False)


# --- gear blank outline -------------------------------------------------------
heel_root = meridian(A, -DED)
toe_root = meridian(Li, -DED * k_toe)
Y_BACK = heel_root[1] + BACK_LAND
R_BACK = heel_root[0] - BACK_LAND * math.tan(DELTA)
FRONT_Y = toe_root[1]          # flat front face starts at the toe root

# envelope that trims every tooth: toe cone, face cone, back cone, back face
toe_lo = meridian(Li, -(DED + 3.0) * k_toe)
heel_lo = meridian(A, -(DED + 3.0))
t_back = (Y_BACK - Y_APEX) / (heel_lo[1] - Y_APEX)
back_lo = (t_back * heel_lo[0], Y_BACK)
heel_tip = meridian(A, ADD)
toe_tip = meridian(Li, ADD * k_toe)
env = (
    cq.Workplane("XY")
    .polyline([toe_lo, back_lo, (R_BACK, Y_BACK), heel_tip, toe_tip])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)

# --- body of revolution: back face, root cone, front face and hub ------------
y_collar_end = TOE_TIP_Y - COLLAR_L
y_neck_end = y_collar_end - NECK_L
y_spline_end = y_neck_end - SPLINE_L
y_end = y_spline_end - FLARE_L
CORE_R = SPLINE_ROOT_R - 0.4

profile = [
    (0.0, Y_BACK),
    (R_BACK, Y_BACK),
    heel_root,
    toe_root,
    (COLLAR_R, FRONT_Y),
    (COLLAR_R, y_collar_end),
    (SPLINE_R, y_neck_end),
    (CORE_R, y_neck_end),
    (CORE_R, y_spline_end),
    (SPLINE_R, y_spline_end),
    (END_R, y_end),
    (0.0, y_end),
]
body = (
    cq.Workplane("XY")
    .polyline(profile)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)

# splined shaft section: rounded ridges (arc profile) extruded along -Y
pitch_a = 2.0 * math.pi / N_SPLINES
sp = cq.Workplane("XZ", origin=(0, y_neck_end, 0))
a0 = -0.5 * pitch_a
sp = sp.moveTo(SPLINE_ROOT_R * math.cos(a0), SPLINE_ROOT_R * math.sin(a0))
for i in range(N_SPLINES):
    ac = i * pitch_a
    ae = (i + 0.5) * pitch_a
    sp = sp.threePointArc(
        (SPLINE_R * math.cos(ac), SPLINE_R * math.sin(ac)),
        (SPLINE_ROOT_R * math.cos(ae), SPLINE_ROOT_R * math.sin(ae)),
    )
spline = sp.close().extrude(SPLINE_L)
body = body.union(spline)

# --- teeth: one trimmed tooth, polar pattern, fused to the body ---------------
tooth = cq.Workplane("XY").add(make_tooth(PHASE)).intersect(env).val()
teeth = [
    tooth.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), -360.0 * i / Z_TEETH)
    for i in range(Z_TEETH)
]

result = body.union(cq.Workplane("XY").add(teeth), clean=False)

VIEW = {"azimuth": 45, "elevation": 26}
